import math
import cadquery as cq

# ---- driving dimensions (mm) ----
# outside
D_OUT = 60.0        # outer diameter of the cap body
BODY_DEPTH = 13.6   # axial depth of the main body (front face -> open back)
D_DISC = 45.2       # diameter of the raised front disc
DISC_H = 7.8        # protrusion of the front disc
R_OUT_FRONT = 2.2   # round on the front outer edge
R_OUT_BACK = 2.7    # full round on the back (mouth) edge
R_BASE = 2.9        # concave fillet where the disc meets the front face
R_DISC = 1.0        # round on the disc front edge
# inside (cavity opened from the back)
SIDE_WALL = 2.7     # side wall of the body (= back round -> full-round lip)
FRONT_WALL = 0.5    # thickness of the front face (annulus around the disc)
DISC_FACE = 1.5     # thickness of the raised disc's face
DISC_WALL = 2.3     # side wall of the raised disc
R_IN = 1.0          # small fillets on the inner corners
SEAM_ANGLE = 135.0  # where the revolve seam sits (deg about the axis)

R = D_OUT / 2.0
RD = D_DISC / 2.0
B = BODY_DEPTH
H = DISC_H
rf, rk, rb, rd = R_OUT_FRONT, R_OUT_BACK, R_BASE, R_DISC
ri = R - SIDE_WALL          # bore radius of the cavity
rr = RD - DISC_WALL         # radius of the inner recess (inside the disc)
y1 = FRONT_WALL             # cavity floor
y3 = -H + DISC_FACE         # recess bottom
c = R_IN


def arc(wp, ctr, rad, a0, a1, end):
    """arc about centre ctr, passing through its angular mid point, ending at `end`."""
    am = math.radians((a0 + a1) / 2.0)
    mid = (ctr[0] + rad * math.cos(am), ctr[1] + rad * math.sin(am))
    return wp.threePointArc(mid, end)


# half cross-section in (radius = X, axial = Y), revolved about the Y axis.
# The raised disc faces -Y (front), the open mouth faces +Y (back).
w = cq.Workplane("XY").moveTo(0, -H)
# --- outer skin: front disc -> mouth ---
w = w.lineTo(RD - rd, -H)
w = arc(w, (RD - rd, -H + rd), rd, -90, 0, (RD, -H + rd))
w = w.lineTo(RD, -rb)
w = arc(w, (RD + rb, -rb), rb, 180, 90, (RD + rb, 0))
w = w.lineTo(R - rf, 0)
w = arc(w, (R - rf, rf), rf, -90, 0, (R, rf))
w = w.lineTo(R, B - rk)
if ri <= R - rk + 1e-6:
    # wall thicker than the back round: full round, then a flat rim to the bore
    w = arc(w, (R - rk, B - rk), rk, 0, 90, (R - rk, B))
    if ri < R - rk - 1e-6:
        w = w.lineTo(ri, B)
else:
    # thinner wall: the back round runs into the bore, leaving a sharp lip
    phi = math.degrees(math.acos((ri - (R - rk)) / rk))
    w = arc(w, (R - rk, B - rk), rk, 0, phi,
            (ri, B - rk + rk * math.sin(math.radians(phi))))
# --- cavity: mouth -> floor -> recess ---
w = w.lineTo(ri, y1 + c)
w = arc(w, (ri - c, y1 + c), c, 0, -90, (ri - c, y1))
w = w.lineTo(rr + c, y1)
w = arc(w, (rr + c, y1 - c), c, 90, 180, (rr, y1 - c))
w = w.lineTo(rr, y3 + c)
w = arc(w, (rr - c, y3 + c), c, 0, -90, (rr - c, y3))
w = w.lineTo(0, y3)
w = w.close()

body = w.revolve(360, (0, 0, 0), (0, 1, 0))
# turn the (cosmetic) revolve seam to the lower back-left, away from the main view
result = body.rotate((0, 0, 0), (0, 1, 0), SEAM_ANGLE)

VIEW = {"azimuth": 45, "elevation": 26}
